import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 260.0          # bar length (along Y)
W = 35.0           # bar width (along X)
H = 9.5            # standard bar thickness
PITCH = 41.0       # bar-to-bar pitch along X
N_STD = 5          # number of identical flat bars
R_EDGE = 1.5       # fillet on long edges of the flat bars

# counterbored through holes near the bar ends
END_HOLE_X = 17.0          # from the -X edge of the bar
END_HOLE_Y = 36.0          # from each bar end
CB_D = 15.0                # counterbore diameter
CB_DEPTH = 7.5             # counterbore depth
THRU_D = 7.5               # through hole diameter
BOT_CH = 1.0               # chamfer where the through hole exits the underside
RIM_CH = 0.75              # small chamfer on hole rims

# blind pockets (same size as the counterbore) further in, toward +X
IN_HOLE_X = 25.0
IN_HOLE_Y = 67.0
BLIND_D = 15.0
BLIND_DEPTH = 7.5

# rounded edge cove along the +X top edge between the blind pockets
COVE_TIP_Y = 77.0          # where the cove starts, from each bar end
COVE_W = 4.9               # width of the cove on the top face
COVE_D = 4.4               # depth of the cove on the side face

# the special L-section edge bar
T_H = 12.0                 # height of the tall part
F_H = 4.7                  # flange height
F_W = 17.0                 # flange width (on the -X side)
CH_BOT = 2.0               # chamfers on the bottom outer corners
POCKET_LEN = 60.0          # central relief in the flange
POCKET_FLOOR = 2.4         # remaining flange thickness in the relief
EDGE_BAR_DY = 1.0          # edge bar sits slightly further back (+Y)

# cove cylinder: axis on the +X edge line, slightly above the top face
COVE_B = (COVE_W ** 2 - COVE_D ** 2) / (2.0 * COVE_D)
COVE_R = COVE_D + COVE_B


def hole_tool(x, y, top, d_bore, depth, d_thru=None):
    """Counterbore / blind bore with a small rim chamfer (+ optional through hole)."""
    r = d_bore / 2.0
    cone = cq.Solid.makeCone(r, r + RIM_CH + 1.0, RIM_CH + 1.0,
                             pnt=cq.Vector(x, y, top - RIM_CH))
    bore = cq.Solid.makeCylinder(r, depth, pnt=cq.Vector(x, y, top - depth))
    tool = cone.fuse(bore)
    if d_thru is not None:
        rt = d_thru / 2.0
        thru = cq.Solid.makeCylinder(rt, top + 2.0, pnt=cq.Vector(x, y, -1.0))
        # matching small chamfer where the through hole leaves the underside
        bot = cq.Solid.makeCone(rt + BOT_CH + 1.0, rt, BOT_CH + 1.0,
                                pnt=cq.Vector(x, y, -1.0))
        tool = tool.fuse(thru).fuse(bot)
    return tool


def cove_tool(x_edge, top, y0, y1):
    """Capsule (ball-end path) running along Y on the top +X edge."""
    zc = top + COVE_B
    ya = y0 + COVE_W   # sphere centres so the tips on the top face land at y0 / y1
    yb = y1 - COVE_W
    cyl = cq.Solid.makeCylinder(COVE_R, yb - ya, pnt=cq.Vector(x_edge, ya, zc),
                                dir=cq.Vector(0, 1, 0))
    s0 = cq.Solid.makeSphere(COVE_R, pnt=cq.Vector(x_edge, ya, zc), angleDegrees1=-90, angleDegrees2=90)
    s1 = cq.Solid.makeSphere(COVE_R, pnt=cq.Vector(x_edge, yb, zc), angleDegrees1=-90, angleDegrees2=90)
    return cyl.fuse(s0).fuse(s1)


def std_bar(x0):
    bar = (cq.Workplane("XY")
           .box(W, L, H, centered=(False, True, False))
           .translate((x0, 0, 0))
           .edges("|Y").fillet(R_EDGE))
    for sy in (-1, 1):
        ye = sy * (L / 2.0 - END_HOLE_Y)
        yi = sy * (L / 2.0 - IN_HOLE_Y)
        bar = bar.cut(hole_tool(x0 + END_HOLE_X, ye, H, CB_D, CB_DEPTH, THRU_D))
        bar = bar.cut(hole_tool(x0 + IN_HOLE_X, yi, H, BLIND_D, BLIND_DEPTH))
    y0 = -L / 2.0 + COVE_TIP_Y
    y1 = L / 2.0 - COVE_TIP_Y
    bar = bar.cut(cove_tool(x0 + W, H, y0, y1))
    return bar


def edge_bar(x0, dy):
    prof = [(0, 0), (W, 0), (W, T_H), (F_W, T_H), (F_W, F_H), (0, F_H)]
    bar = (cq.Workplane("XZ")
           .polyline(prof).close()
           .extrude(-L)                      # XZ normal is -Y, so extrude toward +Y
           .translate((x0, -L / 2.0 + dy, 0)))
    # sharp top edges, chamfers on the two outer bottom edges
    bar = bar.edges("|Y").edges(cq.selectors.NearestToPointSelector((x0, 0, 0))).chamfer(CH_BOT)
    bar = bar.edges("|Y").edges(cq.selectors.NearestToPointSelector((x0 + W, 0, 0))).chamfer(CH_BOT)
    for sy in (-1, 1):
        yi = dy + sy * (L / 2.0 - IN_HOLE_Y)
        bar = bar.cut(hole_tool(x0 + IN_HOLE_X, yi, T_H, BLIND_D, BLIND_DEPTH))
    y0 = dy - L / 2.0 + COVE_TIP_Y
    y1 = dy + L / 2.0 - COVE_TIP_Y
    bar = bar.cut(cove_tool(x0 + W, T_H, y0, y1))
    # central relief lowering the flange
    pocket = (cq.Workplane("XY")
              .box(F_W + 2.0, POCKET_LEN, F_H, centered=(False, True, False))
              .translate((x0 - 2.0, dy, POCKET_FLOOR)))
    bar = bar.cut(pocket)
    return bar


x_start = -(N_STD * PITCH + W) / 2.0
parts = [std_bar(x_start + i * PITCH) for i in range(N_STD)]
parts.append(edge_bar(x_start + N_STD * PITCH, EDGE_BAR_DY))

result = parts[0]
for p in parts[1:]:
    result = result.union(p)

VIEW = {"azimuth": 45, "elevation": 26}
